import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L_TOTAL = 120.0        # overall length along Y (tube end -> disc back)
R_TUBE = 7.75          # outer radius of socket tube at the front end
R_BORE = 5.4           # bore radius of the socket
BORE_DEPTH = 25.0      # blind bore depth
L_TUBE = 27.0          # straight length of socket tube
L_TAPER = 9.0          # taper length from tube to shaft
R_SHAFT = 5.2          # shaft radius
Y_SHAFT_END = 100.6    # where the shaft meets the flare cone
R_FLARE = 12.7         # radius where flare cone meets disc front cone
Y_FLARE = 113.9        # axial position of that junction
R_DISC = 25.3          # disc outer radius
T_RIM = 2.0            # rim (edge) thickness of the disc
R_BOSS = 4.0           # small boss on disc back
H_BOSS = 0.6
R_BOSS_RECESS = 2.7
D_BOSS_RECESS = 1.1
F_BOSS = 0.25          # small round on the boss top edge

F_END = 1.1            # fillet on tube end outer edge
F_BORE = 1.1           # fillet on bore mouth
F_RIM = 1.3            # fillet on disc rim front edge
F_RIM_BACK = 0.9       # fillet on disc rim back edge
F_FLARE_SHAFT = 4.0    # fillet where flare meets shaft
F_FLARE_DISC = 5.5     # fillet where flare meets disc front
F_TAPER = 2.0          # fillets at both ends of the tube->shaft taper

y_rim = L_TOTAL - T_RIM

# profile in (radius=X, axial=Y), revolved about the Y axis
pts = [
    (R_BORE, 0.0),
    (R_TUBE, 0.0),
    (R_TUBE, L_TUBE),
    (R_SHAFT, L_TUBE + L_TAPER),
    (R_SHAFT, Y_SHAFT_END),
    (R_FLARE, Y_FLARE),
    (R_DISC, y_rim),
    (R_DISC, L_TOTAL),
    (0.0, L_TOTAL),
    (0.0, BORE_DEPTH),
    (R_BORE, BORE_DEPTH),
]

body = (
    cq.Workplane("XY")
    .polyline(pts)
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
)


# edge treatment: circular edges picked by (radius, axial position)
def circ_edges(solid, r, y, tol=0.05):
    out = []
    for e in solid.Edges():
        if e.geomType() != "CIRCLE":
            continue
        c = e.Center()
        if abs(e.radius() - r) < tol and abs(c.y - y) < tol:
            out.append(e)
    return out


def fil(wp, r, y, rad):
    s = wp.val()
    return cq.Workplane("XY").add(s.fillet(rad, circ_edges(s, r, y)))


body = fil(body, R_TUBE, 0.0, F_END)
body = fil(body, R_BORE, 0.0, F_BORE)
body = fil(body, R_SHAFT, Y_SHAFT_END, F_FLARE_SHAFT)
body = fil(body, R_FLARE, Y_FLARE, F_FLARE_DISC)
body = fil(body, R_DISC, y_rim, F_RIM)
body = fil(body, R_DISC, L_TOTAL, F_RIM_BACK)
body = fil(body, R_TUBE, L_TUBE, F_TAPER)
body = fil(body, R_SHAFT, L_TUBE + L_TAPER, F_TAPER)

# small boss with a shallow spherical dimple on the disc back face
# ("XZ" workplane normal is -Y, so a negative extrude goes towards +Y)
boss = (
    cq.Workplane("XZ", origin=(0, L_TOTAL, 0))
    .circle(R_BOSS)
    .extrude(-H_BOSS)
)
body = body.union(boss)
body = fil(body, R_BOSS, L_TOTAL + H_BOSS, F_BOSS)

# spherical dimple: sphere meeting the boss top at R_BOSS_RECESS with depth D_BOSS_RECESS
r_sph = (R_BOSS_RECESS ** 2 + D_BOSS_RECESS ** 2) / (2.0 * D_BOSS_RECESS)
y_top = L_TOTAL + H_BOSS
dimple = cq.Workplane("XY").sphere(r_sph).translate((0, y_top - D_BOSS_RECESS + r_sph, 0))
body = body.cut(dimple)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
